import math
import numpy as np
import cadquery as cq
from OCP.GeomAPI import GeomAPI_Interpolate
from OCP.Geom import Geom_BSplineSurface, Geom_BSplineCurve
from OCP.TColgp import TColgp_HArray1OfPnt, TColgp_Array2OfPnt, TColgp_Array1OfPnt
from OCP.TColStd import (TColStd_HArray1OfReal, TColStd_Array1OfReal,
                         TColStd_Array1OfInteger)
from OCP.gp import gp_Pnt
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeFace, BRepBuilderAPI_MakeEdge

# ---------------- driving dimensions (mm) ----------------
LENGTH = 100.0        # nose tip to tail tip (X)
HEIGHT = 36.0         # overall height (Z)
CUT_Z0 = 24.65        # 45-deg nose undercut: height at the nose tip
CUT_X0 = 25.07        # 45-deg nose undercut: X where it reaches the base
HOLE_X = 36.2         # vertical through hole (from nose tip)
HOLE_Y = 3.3
HOLE_D = 8.6

X_SHIFT = -LENGTH / 2.0   # centre the part on the origin

# flank flare profiles (fraction of the way from top outline to base outline)
SIDE_Z_HI, SIDE_Z_LO = 22.6, 4.0                    # long flanks: vertical, late S-flare
FLARE_TAIL = [HEIGHT, 27.4, 19.3, 19.3, 4.6, 0.0]   # tail: quintic blend rows, flare starts high
TAIL_X0, TAIL_X1 = 66.0, 80.0                        # blend (by top X) between the profiles

V_SPANS = 10          # spans of the cubic B-spline up the wall
WALL_SPLITS = [0, 6, 15, 21, 25]   # outline stations where the wall face is split
SMOOTH = 0.02         # fairing weight for the wall fit

# top face outline (z = HEIGHT), CCW, starting at the front of the nose tip
TOP = [
    (0.78, -5.86), (3.23, -7.8), (7.1, -9.74), (10.98, -11.47), (15.87, -13.15),
    (18.78, -13.8), (21.69, -14.38), (26.58, -14.84), (31.09, -15.09), (38.72, -14.38),
    (43.57, -13.15), (48.46, -11.68), (53.31, -9.99), (58.2, -8.26), (62.16, -7.0),
    (64.0, -6.3), (65.79, -5.52), (69.46, -2.95), (73.08, -0.04), (76.04, 2.49),
    (78.6, 4.51), (79.37, 6.96), (78.86, 8.9), (77.17, 11.09), (74.2, 13.03),
    (70.34, 14.76), (65.45, 15.47), (58.2, 15.6), (48.46, 14.97), (38.72, 14.0),
    (31.09, 12.56), (24.14, 11.59), (19.29, 10.62), (14.4, 9.4), (10.52, 7.93),
    (8.07, 5.99), (4.66, 2.07), (2.21, 0.46), (0.53, -1.48), (0.06, -3.41),
]

# base outline (z = 0) before the nose undercut, same count / order as TOP
BOT = [
    (1.0, -6.8), (3.6, -9.6), (7.5, -12.0), (11.3, -13.8), (15.9, -16.3),
    (18.8, -18.3), (21.7, -19.1), (26.6, -20.25), (31.1, -20.55), (38.7, -20.0),
    (43.6, -18.8), (48.5, -17.3), (53.3, -15.35), (58.2, -13.15), (62.2, -10.62),
    (64.4, -9.2), (65.6, -7.9), (69.5, -5.9), (76.8, -3.16), (86.0, 0.2),
    (95.0, 3.8), (100.0, 8.26), (98.6, 11.3), (94.3, 12.6), (85.0, 15.5),
    (75.2, 18.3), (65.5, 20.4), (58.2, 20.7), (48.5, 20.3), (38.7, 19.35),
    (31.1, 18.4), (24.2, 16.8), (19.3, 14.7), (14.4, 12.1), (10.6, 9.3),
    (8.0, 6.9), (4.6, 2.5), (2.1, 0.7), (0.5, -1.3), (0.3, -3.0),
]


def _params(a, b):
    """common spline parameters: mean of the normalised chord lengths."""
    def chords(p):
        n = len(p)
        d = [math.dist(p[i], p[(i + 1) % n]) for i in range(n)]
        t = [0.0]
        for v in d:
            t.append(t[-1] + v)
        return [x / t[-1] for x in t]
    ca, cb = chords(a), chords(b)
    return [(u + v) / 2.0 for u, v in zip(ca, cb)]


PARAMS = _params(TOP, BOT)


def _interp(pts):
    arr = TColgp_HArray1OfPnt(1, len(pts))
    for i, (x, y) in enumerate(pts):
        arr.SetValue(i + 1, gp_Pnt(x, y, 0.0))
    par = TColStd_HArray1OfReal(1, len(PARAMS))
    for i, v in enumerate(PARAMS):
        par.SetValue(i + 1, v)
    b = GeomAPI_Interpolate(arr, par, True, 1e-7)
    b.Perform()
    return b.Curve()


def _smooth(t):
    t = min(1.0, max(0.0, t))
    return t * t * (3 - 2 * t)


# ---- cubic B-spline basis up the wall (v = 1 - z / HEIGHT) ----
V_DEG = 3
V_KNOTS = [0.0] * V_DEG + [i / V_SPANS for i in range(V_SPANS + 1)] + [1.0] * V_DEG
V_ROWS = len(V_KNOTS) - V_DEG - 1
V_GREV = [sum(V_KNOTS[k + 1:k + 1 + V_DEG]) / V_DEG for k in range(V_ROWS)]


def _basis(v):
    kn = V_KNOTS
    n = len(kn) - 1
    N = [1.0 if (kn[i] <= v < kn[i + 1]) or (v >= 1.0 and kn[i] < 1.0 <= kn[i + 1]) else 0.0
         for i in range(n)]
    for d in range(1, V_DEG + 1):
        M = []
        for i in range(n - d):
            a = 0.0
            if kn[i + d] > kn[i]:
                a += (v - kn[i]) / (kn[i + d] - kn[i]) * N[i]
            if kn[i + d + 1] > kn[i + 1]:
                a += (kn[i + d + 1] - v) / (kn[i + d + 1] - kn[i + 1]) * N[i + 1]
            M.append(a)
        N = M
    return N


_ZS = np.linspace(0.0, HEIGHT, 73)
_A = np.array([_basis(1.0 - z / HEIGHT) for z in _ZS])
_TT = np.linspace(0.0, 1.0, 801)
_BERN = np.array([math.comb(5, k) * _TT ** k * (1 - _TT) ** (5 - k) for k in range(6)])
_FRAC = _BERN[3] + _BERN[4] + _BERN[5]
_TAIL_Z = sum(FLARE_TAIL[k] * _BERN[k] for k in range(6))
_SLOPE = CUT_Z0 / CUT_X0


def _column_path(T, B, tau):
    """wall path (x, y at each _ZS) from top pole T to base pole B, with the
    45-degree nose undercut applied."""
    s = np.clip((SIDE_Z_HI - _ZS) / (SIDE_Z_HI - SIDE_Z_LO), 0.0, 1.0)
    f_side = s * s * (3 - 2 * s)
    f_tail = np.interp(_ZS, _TAIL_Z[::-1], _FRAC[::-1])
    f = (1 - tau) * f_side + tau * f_tail
    x = T[0] + f * (B[0] - T[0])
    y = T[1] + f * (B[1] - T[1])
    g = _ZS - CUT_Z0 * (1.0 - x / CUT_X0)        # < 0 : below the undercut plane
    if g.min() < 0.0:
        # first crossing coming down from the top
        idx = np.where(g < 0.0)[0].max()
        i0, i1 = idx, idx + 1
        w = g[i1] / (g[i1] - g[i0])
        zs = _ZS[i1] + w * (_ZS[i0] - _ZS[i1])
        xs = x[i1] + w * (x[i0] - x[i1])
        ys = y[i1] + w * (y[i0] - y[i1])
        low = _ZS < zs
        x = np.where(low, xs + (zs - _ZS) / _SLOPE, x)
        y = np.where(low, ys, y)
    return x, y


def _fit_column(T, path):
    """least-squares cubic B-spline up the wall; rows 0,1 pinned to the top
    pole (vertical start), last row pinned to the path end."""
    x, y = path
    R = V_ROWS
    free = list(range(2, R - 1))
    Af = _A[:, free]
    D = np.zeros((len(free) - 2, len(free)))
    for i in range(len(free) - 2):
        D[i, i:i + 3] = [1.0, -2.0, 1.0]
    out = []
    for comp, tv, ev in ((x, T[0], x[0]), (y, T[1], y[0])):
        rhs = comp - _A[:, 0] * tv - _A[:, 1] * tv - _A[:, R - 1] * ev
        M = np.vstack([Af, SMOOTH * D])
        r = np.concatenate([rhs, np.zeros(D.shape[0])])
        sol = np.linalg.lstsq(M, r, rcond=None)[0]
        poles = [tv, tv] + list(sol) + [ev]
        out.append(poles)
    return list(zip(out[0], out[1]))


def _interp_pts(pts, params):
    arr = TColgp_HArray1OfPnt(1, len(pts))
    for i, (x, y) in enumerate(pts):
        arr.SetValue(i + 1, gp_Pnt(x, y, 0.0))
    par = TColStd_HArray1OfReal(1, len(params))
    for i, v in enumerate(params):
        par.SetValue(i + 1, v)
    b = GeomAPI_Interpolate(arr, par, True, 1e-7)
    b.Perform()
    return b.Curve()


def lofted_body():
    ct = _interp(TOP)
    cb = _interp(BOT)
    # wall stations: the outline points plus the mid-parameters between them
    U = []
    for i in range(len(PARAMS) - 1):
        U += [PARAMS[i], 0.5 * (PARAMS[i] + PARAMS[i + 1])]
    cols = []
    for u in U:
        pt, pb = ct.Value(u), cb.Value(u)
        T, B = (pt.X(), pt.Y()), (pb.X(), pb.Y())
        tau = _smooth((T[0] - TAIL_X0) / (TAIL_X1 - TAIL_X0))
        cols.append(_fit_column(T, _column_path(T, B, tau)))
    # one periodic curve per control row through the station values
    rows = [_interp_pts([c[k] for c in cols], U + [1.0]) for k in range(V_ROWS)]
    c0 = rows[0]
    nu = c0.NbPoles()
    poles = TColgp_Array2OfPnt(1, nu, 1, V_ROWS)
    for k, rc in enumerate(rows):
        for j in range(1, nu + 1):
            p = rc.Pole(j)
            poles.SetValue(j, k + 1, gp_Pnt(p.X() + X_SHIFT, p.Y(), HEIGHT * (1 - V_GREV[k])))
    nk = c0.NbKnots()
    uk = TColStd_Array1OfReal(1, nk)
    um = TColStd_Array1OfInteger(1, nk)
    for i in range(1, nk + 1):
        uk.SetValue(i, c0.Knot(i))
        um.SetValue(i, c0.Multiplicity(i))
    vd = sorted(set(V_KNOTS))
    vk = TColStd_Array1OfReal(1, len(vd))
    vm = TColStd_Array1OfInteger(1, len(vd))
    for i, v in enumerate(vd):
        vk.SetValue(i + 1, v)
        vm.SetValue(i + 1, V_KNOTS.count(v))
    surf = Geom_BSplineSurface(poles, uk, vk, um, vm, c0.Degree(), V_DEG, True, False)
    # the wall is one B-spline surface, trimmed into a few strips (nose tip,
    # front crease, tail tip, back) so that it tessellates faithfully
    cuts = [PARAMS[i] for i in WALL_SPLITS] + [1.0]
    sides = [cq.Face(BRepBuilderAPI_MakeFace(surf, cuts[i], cuts[i + 1], 0.0, 1.0, 1e-7).Face())
             for i in range(len(cuts) - 1)]

    def cap(row, z):
        arr = TColgp_Array1OfPnt(1, nu)
        for j in range(1, nu + 1):
            p = rows[row].Pole(j)
            arr.SetValue(j, gp_Pnt(p.X() + X_SHIFT, p.Y(), z))
        c = Geom_BSplineCurve(arr, uk, um, c0.Degree(), True)
        e = cq.Edge(BRepBuilderAPI_MakeEdge(c).Edge())
        return cq.Face.makeFromWires(cq.Wire.assembleEdges([e]))

    shell = cq.Shell.makeShell(sides + [cap(0, HEIGHT), cap(V_ROWS - 1, 0.0)])
    return cq.Solid.makeSolid(shell)


body = cq.Workplane("XY").add(lofted_body())

# vertical through hole
hole = (
    cq.Workplane("XY")
    .center(HOLE_X + X_SHIFT, HOLE_Y)
    .circle(HOLE_D / 2)
    .extrude(HEIGHT * 3)
    .translate((0, 0, -HEIGHT))
)
result = body.cut(hole, clean=False)

VIEW = {"azimuth": 45, "elevation": 26}
